import math
import cadquery as cq
from OCP.BRepOffsetAPI import BRepOffsetAPI_MakeFilling
from OCP.GeomAbs import GeomAbs_C0
from OCP.gp import gp_Pnt
from OCP.BRep import BRep_Tool
from OCP.GeomAdaptor import GeomAdaptor_Surface
from OCP.BRepBuilderAPI import BRepBuilderAPI_Sewing

# ---------------- driving dimensions (mm) ----------------
LEN = 120.0          # overall length of the oval body (Y)
WID = 75.0           # overall width of the oval body (X)
RIM_Z = 3.7          # height of the rim (where bottom dome meets crown)
TOP_H = 15.5         # crown height of the upper surface
TOP_EXP = 3.0        # super-ellipse exponent of the crown profile
DOME_EXP = 2.7       # profile exponent of the shallow bottom dome

FLOOR_Z = 4.4        # pocket floor height
PK_XL = -22.2        # pocket left straight wall
PK_XR = 19.6         # pocket right straight wall
PK_YC = 5.0          # y where the straight walls turn into the end ellipse
PK_B = 50.0          # semi-axis (Y) of the pocket's +Y end ellipse
PK_CORNER_Y = -24.7  # left wall turns into the diagonal wall here
PK_DIAG_END = (-13.1, -48.0)   # end of diagonal wall
PK_JOG = (-10.4, -48.7)        # small jog before the -Y end arc
PK_ARC_MID = (-6.1, -52.4)
PK_ARC_END = (-0.8, -54.3)     # then straight back to the right wall
PK_RIGHT_Y = -48.3             # -Y end of the right wall

BLK_X0, BLK_X1 = 21.1, 29.5      # mounting block X span (mirrored)
BLK_Y0, BLK_Y1 = 23.8, 36.1      # mounting block Y span
BLK_TOP = 28.6
HOLE_D = 2.9
HOLES = [(32.9, 24.4), (26.8, 18.9), (32.9, 13.7)]   # (Y, Z) through X

TAB_T = 4.2          # clip loop thickness (X)
TAB_W = 12.2         # clip loop width (Y)
TAB_TOP = 18.2
TAB_BOT = 11.4       # bottom of the loop's inner (pocket side) face
TAB_PROUD = 0.2      # loops stand slightly proud of the pocket wall
STEM_W = 1.3         # rib running from the floor up to the loop
STEM_DY = -4.5       # rib offset (Y) from the loop centre
WIN_W = 9.3
WIN_Z0, WIN_Z1 = 14.1, 16.9
TAB_YS = [-21.0, 10.6]

PIN_DY = 12.2        # pins are slightly oval in section
PIN_DZ = 10.6
PIN_Y = -24.2
PIN_Z = 7.65
PIN_X = 36.0         # outer end of the pins
PIN_XI = 22.0        # inner end of the pins

A = WID / 2.0
B = LEN / 2.0


def oval(t, z, start):
    """Closed elliptical wire scaled by t at height z; `start` (deg, parametric
    angle of the ellipse) is where the closed curve begins."""
    e = cq.Edge.makeEllipse(A * t, B * t, cq.Vector(0, 0, z), cq.Vector(0, 0, 1),
                            cq.Vector(1, 0, 0), start, start + 360.0)
    return cq.Wire.assembleEdges([e])


def crown_z(t):
    return RIM_Z + (TOP_H - RIM_Z) * math.sqrt(max(0.0, 1.0 - t ** TOP_EXP))


# ---------------- body ----------------
# crown: oval sections following a super-ellipse profile.  Every section starts
# on the line y = PIN_Y (x > 0) so the loft's seam runs underneath the +X pin
# and clip loop instead of across the visible crown.
crown_ts = (1.0, 0.99, 0.95, 0.88, 0.75, 0.5)
crown_wires = [oval(t, crown_z(t), math.degrees(math.asin(PIN_Y / (B * t))))
               for t in crown_ts]
crown = cq.Solid.makeLoft(crown_wires)
crown_side = [f for f in crown.Faces() if f.geomType() != "PLANE"][0]
crown_top = [f for f in crown.Faces()
             if f.geomType() == "PLANE" and f.Center().z > RIM_Z + 1.0][0]

# bottom dome: smooth filling surface spanning the rim oval (same rim curve as
# the crown), constrained to an apex at z=0 and two rings of points following
# z = RIM_Z * t**DOME_EXP
rim_edge = crown_wires[0].Edges()[0]
fill = BRepOffsetAPI_MakeFilling(3, 15, 2, False, 1e-5, 1e-4, 1e-2, 0.1, 8, 9)
fill.Add(rim_edge.wrapped, GeomAbs_C0)
fill.Add(gp_Pnt(0, 0, 0))
for t_ring in (0.5, 0.8):
    for k in range(8):
        ang = 2 * math.pi * (k + 0.5 * (t_ring > 0.6)) / 8
        fill.Add(gp_Pnt(t_ring * A * math.cos(ang), t_ring * B * math.sin(ang),
                        RIM_Z * t_ring ** DOME_EXP))
fill.Build()
dome_face = cq.Face(fill.Shape())
# refine the patch's knot vectors (shape unchanged) for a finer tessellation
_srf = GeomAdaptor_Surface(BRep_Tool.Surface_s(dome_face.wrapped)).BSpline()
for _k in range(1, 8):
    _srf.InsertUKnot(_srf.UKnot(1) + (_srf.UKnot(_srf.NbUKnots()) - _srf.UKnot(1)) * _k / 8.0, 1, 1e-9)
    _srf.InsertVKnot(_srf.VKnot(1) + (_srf.VKnot(_srf.NbVKnots()) - _srf.VKnot(1)) * _k / 8.0, 1, 1e-9)

# sew dome + crown into one closed body
sew = BRepBuilderAPI_Sewing(1e-4)
for f in (dome_face, crown_side, crown_top):
    sew.Add(f.wrapped)
sew.Perform()
body_solid = cq.Solid.makeSolid(cq.Shell(sew.SewedShape()))
body = cq.Workplane("XY").add(body_solid.fix())

# ---------------- pocket ----------------
a_pk = (PK_XR - PK_XL) / 2.0
pocket = (
    cq.Workplane("XY")
    .workplane(offset=FLOOR_Z)
    .moveTo(PK_XR, PK_RIGHT_Y)
    .lineTo(PK_XR, PK_YC)
    .ellipseArc(a_pk, PK_B, 0, 180, startAtCurrent=True, sense=1)
    .lineTo(PK_XL, PK_CORNER_Y)
    .lineTo(*PK_DIAG_END)
    .lineTo(*PK_JOG)
    .threePointArc(PK_ARC_MID, PK_ARC_END)
    .close()
    .extrude(40)
)
body = body.cut(pocket)

# ---------------- pins ----------------
for sgn in (-1, 1):
    x0 = sgn * PIN_XI if sgn > 0 else -PIN_X
    pin = (
        cq.Workplane("YZ")
        .workplane(offset=x0)
        .center(PIN_Y, PIN_Z)
        .ellipse(PIN_DY / 2, PIN_DZ / 2)
        .extrude(PIN_X - PIN_XI)
    )
    body = body.union(pin)

# ---------------- mounting blocks with holes ----------------
for sgn in (-1, 1):
    xa, xb = sorted((sgn * BLK_X0, sgn * BLK_X1))
    blk = (
        cq.Workplane("XY")
        .box(xb - xa, BLK_Y1 - BLK_Y0, BLK_TOP - FLOOR_Z, centered=False)
        .translate((xa, BLK_Y0, FLOOR_Z))
    )
    for (hy, hz) in HOLES:
        h = (
            cq.Workplane("YZ")
            .workplane(offset=xa - 0.01)
            .center(hy, hz)
            .circle(HOLE_D / 2)
            .extrude(xb - xa + 0.02)
        )
        blk = blk.cut(h)
    body = body.union(blk)

# ---------------- clip loops ----------------
# rectangular snap loops standing on the pocket rim; the two loops next to the
# pins stand slightly proud of the wall and carry a thin rib down to the floor


def crown_at(x, y):
    return crown_z(math.hypot(x / A, y / B))


for sgn in (-1, 1):
    for i, ty in enumerate(TAB_YS):
        proud = TAB_PROUD if i == 0 else 0.0
        if sgn < 0:
            xa, xb = PK_XL - TAB_T, PK_XL + proud
        else:
            xa, xb = PK_XR - proud, PK_XR + TAB_T
        tab = (
            cq.Workplane("XY")
            .box(xb - xa, TAB_W, TAB_TOP - TAB_BOT, centered=False)
            .translate((xa, ty - TAB_W / 2, TAB_BOT))
        )
        win = (
            cq.Workplane("XY")
            .box(xb - xa + 0.02, WIN_W, WIN_Z1 - WIN_Z0, centered=False)
            .translate((xa - 0.01, ty - WIN_W / 2, WIN_Z0))
        )
        body = body.union(tab.cut(win))
        if i == 0:
            if sgn > 0:
                sx0, sx1 = xa, xa + 1.5
            else:
                sx0, sx1 = xb - 1.5, xb
            stem = (
                cq.Workplane("XY")
                .box(sx1 - sx0, STEM_W, TAB_BOT - FLOOR_Z + 0.5, centered=False)
                .translate((sx0, ty + STEM_DY, FLOOR_Z - 0.2))
            )
            body = body.union(stem)
        # where the rim of the pocket rises into the window opening, clear it
        # down to the window sill (the cut reaches just past the wall)
        x_in = xb if sgn < 0 else xa
        ys = [ty - WIN_W / 2 + k * WIN_W / 6 for k in range(7)]
        if max(crown_at(x_in, y) for y in ys) > WIN_Z0:
            ext = 1.0
            cx0 = xa - 0.01 - (ext if sgn > 0 else 0.0)
            cx1 = xb + 0.01 + (ext if sgn < 0 else 0.0)
            clear = (
                cq.Workplane("XY")
                .box(cx1 - cx0, WIN_W, WIN_Z1 - WIN_Z0, centered=False)
                .translate((cx0, ty - WIN_W / 2, WIN_Z0))
            )
            body = body.cut(clear)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
